import math
import cadquery as cq

# ---------------------------------------------------------------
# Clamp bracket: base plate with two mounting lobes, a tower with a
# split clamp collar (+ cross bolt) on top and a strap cradle in front.
# X: back (0) -> front, Y: symmetric about 0, Z: up (bottom at 0)
# ---------------------------------------------------------------

# ---- base plate ----
BASE_T = 6.9            # base plate thickness
HOLE_X = 49.65          # mounting hole x
HOLE_Y = 22.63          # mounting hole +/- y
HOLE_D = 10.3           # mounting hole diameter
LOBE_R = 9.16           # lobe radius around mounting holes
FRONT_CONC_X = 55.4     # apex of concave front edge between lobes
SIDE_CONC_R = 32.4      # radius of concave side edge (tangent to tower side)
BASE_FIL = 0.8

# ---- tower ----
TOWER_HW = 17.05        # tower half width (y)
BODY_X0 = 4.3           # back of full-width body
BACK_HW = 10.2          # half width of narrow back column
FACE_X = 11.2           # front face of clamp head / ear depth
RING_Z = 34.6           # clamp bore axis height
RING_R = 10.2           # clamp collar outer radius
BORE_D = 11.6           # clamp bore diameter
EAR_HW = 5.7            # outer half width of the two ears
SLOT_W = 3.4            # split slot width
TOP_Z = 51.5            # top of ears
EAR_TOP_R = 1.9         # rounding of ear top corners
EAR_HOLE_D = 4.1        # cross bolt hole
EAR_HOLE_X = 5.6
EAR_HOLE_Z = 47.5
FLARE_C = (26.9, 44.0)  # centre of concave flare from collar to body
EAR_FIL_R = 1.5         # concave fillet where the ears meet the collar
EDGE_R = 0.8            # edge rounding of the cradle rims
HEAD_EDGE_R = 0.6       # edge rounding of the head / ears

# ---- cradle (XZ profile of the side rims) ----
CR_C = (20.0, 16.6)     # cradle circle centre (x, z)
CR_R = 7.0              # cradle radius
WALL_TOP_Z = 27.1       # where cradle back wall meets the head face
WALL_BLEND_R = 8.0      # blend between back wall and head face
FRONT_FOOT_X = 31.4     # foot of sloped front face on base top
FRONT_ANG = 14.8        # front face lean from vertical (deg)
TIP_R = 1.05            # rounded lip tip radius
INNER_DROP = 1.5        # inner cradle (between rims) sits lower
TAB_TOP_Z = 15.0        # flat top of the two inner front tabs
RIM_W = 3.35            # width of side rims

# ---- strap path ----
STRAP_HW = 3.5          # half width of strap channel
WIN_Z0, WIN_Z1 = 15.75, 24.6
BACK_OPEN_Z = 11.0
REC_X0 = 1.0            # back end of the underside recess
NOTCH_X0 = 22.5         # back of front notch / ramp start (on the bottom)
NOTCH_X1 = 33.0         # front end of ramp in the base top
RAMP_Z1 = BASE_T          # ramp height at its front end (meets the base top)


# ================= helpers =================
def arc_mid(c, r, p0, p1, ccw):
    """Mid point of the arc of circle (c, r) from p0 to p1, ccw or cw."""
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    if ccw:
        da = (a1 - a0) % (2 * math.pi)
    else:
        da = -((a0 - a1) % (2 * math.pi))
    am = a0 + da / 2
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


def tangent_point(p, c, r, pick_min_x=True):
    """Tangent point on circle (c, r) seen from external point p."""
    dx, dz = c[0] - p[0], c[1] - p[1]
    d = math.hypot(dx, dz)
    a = math.asin(r / d)
    base = math.atan2(dz, dx)
    L = math.sqrt(d * d - r * r)
    pts = [(p[0] + L * math.cos(base + s * a), p[1] + L * math.sin(base + s * a))
           for s in (1, -1)]
    pts.sort(key=lambda q: q[0])
    return pts[0] if pick_min_x else pts[1]


def _try_fillet(wp, edges, r):
    if not edges:
        return wp
    try:
        shp = wp.val().fillet(r, edges)
        if shp.isValid():
            return cq.Workplane("XY").newObject([shp])
    except Exception:
        pass
    return wp


def _is_parallel_y(e):
    if e.geomType() != "LINE":
        return False
    d = e.endPoint() - e.startPoint()
    return abs(d.x) < 1e-6 and abs(d.z) < 1e-6


# ================= base plate =================
def base_plate():
    lx, ly, lr = HOLE_X, HOLE_Y, LOBE_R
    # concave front arc: centre on x axis, tangent to both lobes
    a = FRONT_CONC_X - lx
    Rf = (a * a + ly * ly - lr * lr) / (2 * (lr - a))
    cf = (FRONT_CONC_X + Rf, 0.0)
    # concave side arc: tangent to the tower side line and to the lobe
    Rs = SIDE_CONC_R
    yl = TOWER_HW - BASE_FIL          # tangent line hidden inside the tower
    sc = (lx - math.sqrt((Rs + lr) ** 2 - (yl + Rs - ly) ** 2), yl + Rs)
    dsl = Rs + lr
    xt = sc[0]
    # tangent points (upper half)
    ts = (sc[0] + (lx - sc[0]) * Rs / dsl, sc[1] + (ly - sc[1]) * Rs / dsl)
    dfl = math.hypot(lx - cf[0], ly)
    tf = (cf[0] + (lx - cf[0]) * Rf / dfl, (ly - 0) * Rf / dfl)

    def m(p):
        return (p[0], -p[1])

    sc_l = m(sc)
    Lu, Ll = (lx, ly), (lx, -ly)
    w = (cq.Workplane("XY")
         .moveTo(BODY_X0 + 2.0, -yl)
         .lineTo(xt, -yl)
         .threePointArc(arc_mid(sc_l, Rs, (xt, -yl), m(ts), False), m(ts))
         .threePointArc(arc_mid(Ll, lr, m(ts), m(tf), True), m(tf))
         .threePointArc((FRONT_CONC_X, 0), tf)
         .threePointArc(arc_mid(Lu, lr, tf, ts, True), ts)
         .threePointArc(arc_mid(sc, Rs, ts, (xt, yl), False), (xt, yl))
         .lineTo(BODY_X0 + 2.0, yl)
         .close())
    plate = w.extrude(BASE_T)
    try:
        plate = plate.faces(">Z").edges().fillet(BASE_FIL)
    except Exception:
        pass
    holes = (cq.Workplane("XY")
             .pushPoints([(lx, ly), (lx, -ly)])
             .circle(HOLE_D / 2).extrude(BASE_T))
    plate = plate.cut(holes)
    sel = [e for e in plate.edges("%CIRCLE").vals()
           if abs(e.Center().z - BASE_T) < 1e-3
           and abs(e.radius() - HOLE_D / 2) < 1e-3]
    plate = _try_fillet(plate, sel, 0.6)
    return plate


# ================= tower =================
def ear_fillet_pts():
    """Tangent points of the concave fillet between ear side and collar."""
    rfe = EAR_FIL_R
    zc = RING_Z + math.sqrt((RING_R + rfe) ** 2 - (EAR_HW + rfe) ** 2)
    c = (EAR_HW + rfe, zc)
    k = RING_R / (RING_R + rfe)
    p_ring = (c[0] * k, RING_Z + (zc - RING_Z) * k)
    p_ear = (EAR_HW, zc)
    mid = arc_mid(c, rfe, p_ring, p_ear, False)
    return p_ring, mid, p_ear


def head_yz(x0, x1, hw_body=TOWER_HW):
    """YZ outline (collar + ears + flare to body) extruded from x0 to x1."""
    fc = FLARE_C
    dfo = math.hypot(fc[0], fc[1] - RING_Z)
    rf = dfo - RING_R
    zs = fc[1] - math.sqrt(rf * rf - (hw_body - fc[0]) ** 2)
    tp = (fc[0] * RING_R / dfo, RING_Z + (fc[1] - RING_Z) * RING_R / dfo)
    oc = (0.0, RING_Z)
    pr, pm, pe = ear_fillet_pts()
    fm = arc_mid(fc, rf, (hw_body, zs), tp, False)
    rm = arc_mid(oc, RING_R, tp, pr, True)
    fc_l = (-fc[0], fc[1])
    fml = arc_mid(fc_l, rf, (-tp[0], tp[1]), (-hw_body, zs), False)
    rml = arc_mid(oc, RING_R, (-pr[0], pr[1]), (-tp[0], tp[1]), True)
    w = (cq.Workplane("YZ", origin=(x0, 0, 0))
         .moveTo(-hw_body, 0)
         .lineTo(hw_body, 0)
         .lineTo(hw_body, zs)
         .threePointArc(fm, tp)
         .threePointArc(rm, pr)
         .threePointArc(pm, pe)
         .lineTo(EAR_HW, TOP_Z)
         .lineTo(-EAR_HW, TOP_Z)
         .lineTo(-pe[0], pe[1])
         .threePointArc((-pm[0], pm[1]), (-pr[0], pr[1]))
         .threePointArc(rml, (-tp[0], tp[1]))
         .threePointArc(fml, (-hw_body, zs))
         .close())
    return w.extrude(x1 - x0)


def collar_yz(x0, x1):
    """Collar ring + ears + narrow back column (tombstone outline)."""
    oc = (0.0, RING_Z)
    pr, pm, pe = ear_fillet_pts()
    m1 = arc_mid(oc, RING_R, (BACK_HW, RING_Z), pr, True)
    m2 = arc_mid(oc, RING_R, (-pr[0], pr[1]), (-BACK_HW, RING_Z), True)
    w = (cq.Workplane("YZ", origin=(x0, 0, 0))
         .moveTo(-BACK_HW, 0)
         .lineTo(BACK_HW, 0)
         .lineTo(BACK_HW, RING_Z)
         .threePointArc(m1, pr)
         .threePointArc(pm, pe)
         .lineTo(EAR_HW, TOP_Z)
         .lineTo(-EAR_HW, TOP_Z)
         .lineTo(-pe[0], pe[1])
         .threePointArc((-pm[0], pm[1]), (-pr[0], pr[1]))
         .threePointArc(m2, (-BACK_HW, RING_Z))
         .close())
    return w.extrude(x1 - x0)


def cradle_geometry(grow=0.0, drop=0.0):
    """Key points of the XZ cradle profile; `grow` enlarges the cradle
    circle and shifts the back wall, `drop` lowers the cradle circle and
    back wall (inner cradle between the rims)."""
    cx, cz = CR_C
    cz -= drop
    R = CR_R + grow
    ang = math.radians(FRONT_ANG)
    u = (-math.sin(ang), math.cos(ang))          # up the front face
    n_in = (-math.cos(ang), -math.sin(ang))      # into the material
    foot = (FRONT_FOOT_X, BASE_T)
    bx = foot[0] + TIP_R * n_in[0] - cx
    bz = foot[1] + TIP_R * n_in[1] - cz
    B = 2 * (bx * u[0] + bz * u[1])
    Cc = bx * bx + bz * bz - (R + TIP_R) ** 2
    s = (-B - math.sqrt(B * B - 4 * Cc)) / 2
    T = (foot[0] + s * u[0] + TIP_R * n_in[0], foot[1] + s * u[1] + TIP_R * n_in[1])
    tip_front = (foot[0] + s * u[0], foot[1] + s * u[1])
    dct = math.hypot(T[0] - cx, T[1] - cz)
    tip_back = (cx + (T[0] - cx) * R / dct, cz + (T[1] - cz) * R / dct)
    tip_mid = arc_mid(T, TIP_R, tip_front, tip_back, True)
    bot = (cx, cz - R)
    # back wall: line tangent to circle, blended into the vertical face
    wall_x = FACE_X - grow
    p = (wall_x, WALL_TOP_Z - drop)
    wt = tangent_point(p, (cx, cz), R, True)
    # blend arc between wall line (wt -> p) and vertical x = wall_x
    dx, dz = p[0] - wt[0], p[1] - wt[1]
    L = math.hypot(dx, dz)
    ux, uz = dx / L, dz / L                  # up the wall
    theta = math.atan2(-ux, uz)             # lean angle from vertical
    t = WALL_BLEND_R * math.tan(theta / 2)
    b0 = (p[0] - ux * t, p[1] - uz * t)     # on wall line
    b1 = (p[0], p[1] + t)                   # on vertical face
    bc = (p[0] + WALL_BLEND_R, p[1] + t)    # blend centre (air side)
    bm = arc_mid(bc, WALL_BLEND_R, b0, b1, False)
    return dict(foot=foot, tip_front=tip_front, tip_mid=tip_mid,
                tip_back=tip_back, bot=bot, wt=wt, b0=b0, bm=bm, b1=b1,
                R=R, T=T, wall_x=wall_x, c=(cx, cz))


def body_xz():
    g = cradle_geometry()
    c = CR_C
    R = g["R"]
    m1 = arc_mid(c, R, g["tip_back"], g["bot"], False)
    m2 = arc_mid(c, R, g["bot"], g["wt"], False)
    w = (cq.Workplane("XZ", origin=(0, TOWER_HW, 0))
         .moveTo(0, 0)
         .lineTo(FRONT_FOOT_X, 0)
         .lineTo(*g["foot"])
         .lineTo(*g["tip_front"])
         .threePointArc(g["tip_mid"], g["tip_back"])
         .threePointArc(m1, g["bot"])
         .threePointArc(m2, g["wt"])
         .lineTo(*g["b0"])
         .threePointArc(g["bm"], g["b1"])
         .lineTo(FACE_X, TOP_Z + 5)
         .lineTo(0, TOP_Z + 5)
         .close())
    return w.extrude(2 * TOWER_HW)


def tower():
    full = body_xz().intersect(head_yz(-1, 40))
    # narrow the back of the tower to the collar (tombstone) outline
    corner = head_yz(-2, BODY_X0).cut(collar_yz(-3, BODY_X0 + 1))
    t = full.cut(corner)
    # rounded vertical corners at the back
    sel = [e for e in t.edges("|Z").vals()
           if (abs(e.Center().x - BODY_X0) < 1e-3 and abs(abs(e.Center().y) - TOWER_HW) < 1e-3)]
    t = _try_fillet(t, sel, 1.5)
    sel = [e for e in t.edges("|Z").vals()
           if (abs(e.Center().x) < 1e-3 and abs(abs(e.Center().y) - BACK_HW) < 1e-3)]
    t = _try_fillet(t, sel, 1.0)
    # rounded top edges of the ears (front and back)
    sel = [e for e in t.edges().vals()
           if _is_parallel_y(e) and abs(e.Center().z - TOP_Z) < 1e-3]
    t = _try_fillet(t, sel, EAR_TOP_R)
    # rounded outline of the cradle rims (each side separately) and head face
    for sgn in (1, -1):
        sel = [e for e in t.edges().vals()
               if abs(e.Center().y - sgn * TOWER_HW) < 1e-3
               and e.Center().x > BODY_X0 + 2.0
               and BASE_T + 0.3 < e.Center().z < TOP_Z - 0.5]
        t = _try_fillet(t, sel, EDGE_R)
    # rounded outline of the head face (the back outline is already rounded
    # by the tangent-chain fillet of the back column corners)
    sel = [e for e in t.edges().vals()
           if abs(e.Center().x - FACE_X) < 1e-3 and not _is_parallel_y(e)
           and BASE_T + 0.3 < e.Center().z < TOP_Z - 0.5]
    t = _try_fillet(t, sel, HEAD_EDGE_R)

    # split slot between ears and clamp bore (axis along X)
    slot = (cq.Workplane("XY")
            .box(FACE_X + 2, SLOT_W, TOP_Z - RING_Z + 2, centered=(False, True, False))
            .translate((-1, 0, RING_Z)))
    t = t.cut(slot)
    bore = (cq.Workplane("YZ", origin=(-1, 0, 0)).center(0, RING_Z)
            .circle(BORE_D / 2).extrude(FACE_X + 2))
    t = t.cut(bore)
    # small rounding where the slot runs into the bore
    sel = [e for e in t.edges("|X").vals()
           if abs(abs(e.Center().y) - SLOT_W / 2) < 1e-3 and e.Center().z < RING_Z + BORE_D / 2 + 0.1]
    t = _try_fillet(t, sel, 0.8)
    # rounded vertical edges of the slot
    sel = [e for e in t.edges("|Z").vals()
           if abs(abs(e.Center().y) - SLOT_W / 2) < 1e-3 and e.Center().z > RING_Z]
    t = _try_fillet(t, sel, HEAD_EDGE_R)
    # cross bolt hole through ears (axis Y)
    eh = (cq.Workplane("XZ", origin=(0, EAR_HW + 1, 0))
          .center(EAR_HOLE_X, EAR_HOLE_Z).circle(EAR_HOLE_D / 2)
          .extrude(2 * EAR_HW + 2))
    t = t.cut(eh)
    return t


def inner_cradle_cut():
    """The cradle between the two side rims sits INNER_DROP lower than the
    rims, so the inner front tabs end below the rounded rim tips."""
    g = cradle_geometry(drop=INNER_DROP)
    c = g["c"]
    R = g["R"]
    hw = TOWER_HW - RIM_W
    m1 = arc_mid(c, R, g["tip_back"], g["bot"], False)
    m2 = arc_mid(c, R, g["bot"], g["wt"], False)
    w = (cq.Workplane("XZ", origin=(0, hw, 0))
         .moveTo(FACE_X, 60)
         .lineTo(*g["b1"])
         .threePointArc(g["bm"], g["b0"])
         .lineTo(*g["wt"])
         .threePointArc(m2, g["bot"])
         .threePointArc(m1, g["tip_back"])
         .threePointArc(g["tip_mid"], g["tip_front"])
         .lineTo(g["tip_front"][0], 60)
         .close())
    cut = w.extrude(2 * hw)
    # flat tops of the inner tabs, below the rounded rim tips
    tab = (cq.Workplane("XY")
           .box(14, 2 * hw, 20, centered=(False, True, False))
           .translate((CR_C[0] + 2.0, 0, TAB_TOP_Z)))
    return cut.union(tab)


def strap_cuts():
    cuts = []
    # window channel from the cradle back wall, descending to the back face
    x_lo, x_hi = 13.2, 11.6
    k = (WIN_Z1 - BACK_OPEN_Z) / x_hi
    xa, xb = -2.0, 17.0
    pts = [(xa, WIN_Z0 + k * (xa - x_lo)), (xb, WIN_Z0 + k * (xb - x_lo)),
           (xb, WIN_Z1 + k * (xb - x_hi)), (xa, WIN_Z1 + k * (xa - x_hi))]
    ch = (cq.Workplane("XZ", origin=(0, STRAP_HW, 0)).polyline(pts).close()
          .extrude(2 * STRAP_HW))
    lim = (cq.Workplane("XY").box(40, 20, WIN_Z1 + 1, centered=(False, True, False))
           .translate((-5, 0, -1)))
    cuts.append(ch.intersect(lim))
    # underside recess: roof rising from the bottom face toward the notch
    cx, cz = CR_C
    rec_h = (cz - INNER_DROP) - math.sqrt(CR_R ** 2 - (NOTCH_X0 - cx) ** 2) - 0.15
    kr = rec_h / (NOTCH_X0 - REC_X0)
    rec = (cq.Workplane("XZ", origin=(0, STRAP_HW, 0))
           .polyline([(REC_X0 - 1.0 / kr, -1), (NOTCH_X0, -1), (NOTCH_X0, rec_h)]).close()
           .extrude(2 * STRAP_HW))
    cuts.append(rec)
    # front notch between the tabs; its floor is a ramp from the bottom
    # face up to the base top in front of the tabs
    ks = RAMP_Z1 / (NOTCH_X1 - NOTCH_X0)
    notch = (cq.Workplane("XZ", origin=(0, STRAP_HW, 0))
             .polyline([(NOTCH_X0, -1), (NOTCH_X0, 40), (NOTCH_X1, 40),
                        (NOTCH_X1, RAMP_Z1), (NOTCH_X0 - 1.0 / ks, -1)]).close()
             .extrude(2 * STRAP_HW))
    cuts.append(notch)
    return cuts


base = base_plate()
tw = tower()
part = tw.union(base)
part = part.cut(inner_cradle_cut())
for c in strap_cuts():
    part = part.cut(c)

# rounded edges of the two front tabs (notch sides and top front edge)
def _pick(wp, cond):
    return [e for e in wp.edges().vals() if cond(e.Center(), e)]


tab_edges = (_pick(part, lambda c, e: e.geomType() == "LINE"
                   and abs(abs(c.y) - STRAP_HW) < 1e-3 and c.x > 29 and 8 < c.z < 14)
             + _pick(part, lambda c, e: e.geomType() == "LINE"
                     and abs(c.z - TAB_TOP_Z) < 1e-3 and c.x > 28.5 and abs(c.y) > 5))
part = _try_fillet(part, tab_edges, 0.6)

result = part

VIEW = {"azimuth": 45, "elevation": 26}
